"""Barbed hose-tail / grommet: a turned part with a through bore, a tapered
top entry cone, three sharp barb ridges with concave (arc + cone) flanks
between them and a concave skirt down to the bottom face.

The outer profile is built in the XZ half-plane (x = radius, z = height)
and revolved about the Z axis."""
import math
import cadquery as cq
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.gp import gp_Pnt

# ---------------- driving dimensions (mm) ----------------
RIDGE_R = 7.0          # radius at the sharp barb ridges
TOP_R = 5.77           # outer radius of the top (narrow) end face
BOTTOM_R = 5.41        # outer radius of the bottom end face
BORE_R = 3.84          # through bore radius
BOTTOM_SEG = 4.0       # height from bottom face to lowest ridge
PITCH = 9.9            # ridge-to-ridge spacing
TOP_SEG = 5.93         # height from top ridge to top face
N_RIDGES = 3
CONE_SLOPE = 0.207     # dr/dz of the barb cone flanks (narrowing upward)
GROOVE_R = 5.12        # radius of the concave arc below each upper ridge
BOTTOM_ARC_R = 6.87    # radius of the concave arc forming the bottom skirt

HEIGHT = BOTTOM_SEG + (N_RIDGES - 1) * PITCH + TOP_SEG
ridge_z = [BOTTOM_SEG + i * PITCH for i in range(N_RIDGES)]


def P3(r, z):
    return gp_Pnt(r, 0.0, z)


def groove_edge(z_low, z_up):
    """One smooth flank between two ridges: a straight cone line rising from
    the lower ridge, blending tangentially into a concave arc (radius
    GROOVE_R) that ends at the upper ridge.  Line + arc are written exactly
    as a single C1 rational quadratic B-spline so the flank is one face."""
    s = CONE_SLOPE
    k = math.sqrt(1 + s * s)
    p = z_up - z_low
    # arc centre (cr, cz): passes through upper ridge, tangent to cone line
    m = GROOVE_R * k - s * p
    disc = (m * s) ** 2 - (1 + s * s) * (m * m - GROOVE_R ** 2)
    b = (m * s - math.sqrt(disc)) / (1 + s * s)
    a = m - s * b
    cr, cz = RIDGE_R + a, z_up + b
    nr, nz = 1 / k, s / k                      # outward unit normal of line
    T = (cr - GROOVE_R * nr, cz - GROOVE_R * nz)  # tangent point
    Pu = (RIDGE_R, z_up)                       # upper ridge
    Ql = (RIDGE_R, z_low)                      # lower ridge
    # arc Bezier: Pu -> K -> T ; K = intersection of the end tangents
    dl = (-s / k, 1 / k)                       # line direction (upwards)
    v = (Pu[0] - cr, Pu[1] - cz)
    tp = (-v[1], v[0])                         # tangent at Pu (either sense)
    # solve T + t*dl = Pu + u*tp
    det = dl[0] * (-tp[1]) - dl[1] * (-tp[0])
    rx, ry = Pu[0] - T[0], Pu[1] - T[1]
    t = (rx * (-tp[1]) - ry * (-tp[0])) / det
    K = (T[0] + t * dl[0], T[1] + t * dl[1])
    cosang = ((v[0]) * (T[0] - cr) + (v[1]) * (T[1] - cz)) / GROOVE_R ** 2
    theta = math.acos(max(-1.0, min(1.0, cosang)))
    wk = math.cos(theta / 2)
    # line Bezier: Ql -> M -> T, M at the middle of the line segment
    M = ((Ql[0] + T[0]) / 2, (Ql[1] + T[1]) / 2)
    # C1 join in homogeneous coords: T = a*K + b*M, a + b = 1 (w_T = 1)
    dKM = math.hypot(M[0] - K[0], M[1] - K[1])
    aa = math.hypot(M[0] - T[0], M[1] - T[1]) / dKM
    bb = 1 - aa
    alpha = aa / wk                 # = span_line / (span_line + span_arc)
    wm = bb / (1 - alpha)
    u1 = alpha                      # knot where line (first) meets arc
    poles = TColgp_Array1OfPnt(1, 4)
    weights = TColStd_Array1OfReal(1, 4)
    for i, (pt, w) in enumerate([(Ql, 1.0), (M, wm), (K, wk), (Pu, 1.0)]):
        poles.SetValue(i + 1, P3(*pt))
        weights.SetValue(i + 1, w)
    knots = TColStd_Array1OfReal(1, 3)
    mults = TColStd_Array1OfInteger(1, 3)
    for i, (kv, mv) in enumerate([(0.0, 3), (u1, 1), (1.0, 3)]):
        knots.SetValue(i + 1, kv)
        mults.SetValue(i + 1, mv)
    curve = Geom_BSplineCurve(poles, weights, knots, mults, 2)
    return cq.Edge(BRepBuilderAPI_MakeEdge(curve).Edge())


def bottom_arc_mid():
    """Mid point of the concave skirt arc from bottom edge to lowest ridge."""
    x1, y1 = BOTTOM_R, 0.0
    x2, y2 = RIDGE_R, BOTTOM_SEG
    mx, my = (x1 + x2) / 2, (y1 + y2) / 2
    dx, dy = x2 - x1, y2 - y1
    d = math.hypot(dx, dy)
    h = math.sqrt(BOTTOM_ARC_R ** 2 - (d / 2) ** 2)
    ux, uy = dy / d, -dx / d
    cx, cy = mx + h * ux, my + h * uy
    if cx < mx:                      # centre on the outside of the part
        cx, cy = mx - h * ux, my - h * uy
    vx, vy = mx - cx, my - cy
    L = math.hypot(vx, vy)
    return (cx + BOTTOM_ARC_R * vx / L, cy + BOTTOM_ARC_R * vy / L)


def V(r, z):
    return cq.Vector(r, 0.0, z)


# ---------------- half profile, revolved about Z ----------------
# (the bore is cut separately; both are axisymmetric, the rotations only
#  park the surface seams of the revolved faces on the hidden back side)
SEAM_ANGLE = 180.0        # deg about Z for the seam of the outer surfaces
BORE_SEAM_ANGLE = 45.0    # deg about Z for the seam of the bore

edges = [
    cq.Edge.makeLine(V(0, 0), V(BOTTOM_R, 0)),
    cq.Edge.makeThreePointArc(V(BOTTOM_R, 0), V(*bottom_arc_mid()),
                              V(RIDGE_R, ridge_z[0])),
]
for i in range(N_RIDGES - 1):
    edges.append(groove_edge(ridge_z[i], ridge_z[i + 1]))
edges += [
    cq.Edge.makeLine(V(RIDGE_R, ridge_z[-1]), V(TOP_R, HEIGHT)),
    cq.Edge.makeLine(V(TOP_R, HEIGHT), V(0, HEIGHT)),
    cq.Edge.makeLine(V(0, HEIGHT), V(0, 0)),
]
profile = cq.Wire.assembleEdges(edges)
body = cq.Solid.revolve(profile, [], 360, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
body = body.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_ANGLE)

# through bore
bore = cq.Solid.makeCylinder(BORE_R, HEIGHT + 2.0, cq.Vector(0, 0, -1.0),
                             cq.Vector(0, 0, 1))
bore = bore.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), BORE_SEAM_ANGLE)

result = cq.Workplane("XY").add(body).cut(cq.Workplane("XY").add(bore))

VIEW = {"azimuth": 45, "elevation": 26}
